import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 206.0          # overall width  (X)
H = 100.0          # overall height (Z)
D = 62.0           # overall depth  (Y), front face at Y=0, open at Y=D
R_CORNER = 8.3     # corner radius of the box (edges along Y)
T_WALL = 2.8       # wall thickness

# top / bottom wall trapezoid cut-out (seen from above)
TB_FRONT_Y = 9.7   # depth of the remaining top/bottom wall strip in the middle
TB_HALF_FRONT = 54.0
TB_HALF_BACK = 78.7
TB_R_IN = 3.0      # concave corner round at the front of the cut-out
TB_R_OUT = 2.5     # convex round at the rear tip of the arms

# side wall trapezoid cut-out (+X end only, seen from the side)
SD_FRONT_Y = 18.0
SD_HALF_FRONT = 26.5
SD_HALF_BACK = 38.0
SD_R_IN = 2.5
SD_R_OUT = 3.0

# corner lugs
LUG_X = 88.5       # lug axis |x|
LUG_DZ = 2.0       # lug axis above the outer wall surface
LUG_R = 5.2
LUG_L = 10.2
LUG_HOLE_R = 1.1
LUG_CHAMFER_Y = 5.9
LUG_POCKET_R = 3.6  # hex pocket (circumradius) on the inclined face
LUG_POCKET_D = 1.8

# groove along the arms
GR_X = 88.85       # groove centre |x|
GR_W = 4.5
GR_DEPTH = 0.7

# inner panel on the front plate
PANEL_HALF_X = 71.5
PANEL_HALF_Z = 36.8
PANEL_T = 1.0

# inner screw bosses (+X end)
BOSS_X = 95.0
BOSS_Z = 40.5
BOSS_R = 5.0
BOSS_HOLE_R = 1.3
BOSS_CSK_R = 2.3
BOSS_FACE_Y = 9.0

LUG_BASE_R = 1.0   # round at the lug foot
REAR_R = 0.8       # round on the rear rim

VIEW = {"azimuth": 45, "elevation": 26}


def box_sel(x0, y0, z0, x1, y1, z1):
    return cq.selectors.BoxSelector((x0, y0, z0), (x1, y1, z1))


# ---------------- main shell ----------------
body = (
    cq.Workplane("XZ")
    .rect(W, H)
    .extrude(-D)               # XZ normal is -Y, so negative extrude goes +Y
    .edges("|Y")
    .fillet(R_CORNER)
)
body = body.faces(">Y").shell(-T_WALL)

# ---------------- top / bottom trapezoid cut ----------------
E = 30.0   # how far the cutter runs past the rear edge / sides
tb_pts = [
    (-TB_HALF_FRONT, TB_FRONT_Y),
    (TB_HALF_FRONT, TB_FRONT_Y),
    (TB_HALF_BACK, D),
    (TB_HALF_BACK + E, D),
    (TB_HALF_BACK + E, D + E),
    (-TB_HALF_BACK - E, D + E),
    (-TB_HALF_BACK - E, D),
    (-TB_HALF_BACK, D),
]
tb_cut = (
    cq.Workplane("XY")
    .workplane(offset=-H)
    .polyline(tb_pts).close()
    .extrude(2 * H)
)
tb_cut = tb_cut.edges(box_sel(-W, TB_FRONT_Y - 1, -2 * H, W, TB_FRONT_Y + 1, 2 * H)).fillet(TB_R_IN)
tb_cut = tb_cut.edges(
    box_sel(-TB_HALF_BACK - 1, D - 1, -2 * H, TB_HALF_BACK + 1, D + 1, 2 * H)
).fillet(TB_R_OUT)
body = body.cut(tb_cut)

# ---------------- side trapezoid cut (+X end only) ----------------
sd_pts = [
    (SD_FRONT_Y, -SD_HALF_FRONT),
    (SD_FRONT_Y, SD_HALF_FRONT),
    (D, SD_HALF_BACK),
    (D, SD_HALF_BACK + E),
    (D + E, SD_HALF_BACK + E),
    (D + E, -SD_HALF_BACK - E),
    (D, -SD_HALF_BACK - E),
    (D, -SD_HALF_BACK),
]
sd_cut = (
    cq.Workplane("YZ")
    .workplane(offset=W / 2 - 10)
    .polyline(sd_pts).close()
    .extrude(20)
)
sd_cut = sd_cut.edges(box_sel(0, SD_FRONT_Y - 1, -H, W, SD_FRONT_Y + 1, H)).fillet(SD_R_IN)
sd_cut = sd_cut.edges(
    box_sel(0, D - 1, -SD_HALF_BACK - 1, W, D + 1, SD_HALF_BACK + 1)
).fillet(SD_R_OUT)
body = body.cut(sd_cut)

# ---------------- inner panel ----------------
panel = (
    cq.Workplane("XZ", origin=(0, T_WALL, 0))
    .rect(2 * PANEL_HALF_X, 2 * PANEL_HALF_Z)
    .extrude(-PANEL_T)
)
body = body.union(panel)

# ---------------- inner bosses (+X end) ----------------
for sz in (-1, 1):
    boss = (
        cq.Workplane("XZ", origin=(BOSS_X, T_WALL, sz * BOSS_Z))
        .circle(BOSS_R)
        .extrude(-(BOSS_FACE_Y - T_WALL))
    )
    # keep the boss inside the shell
    boss = boss.intersect(
        cq.Workplane("XY").box(W - 2 * T_WALL, D, H - 2 * T_WALL, centered=(True, False, True))
    )
    bhole = (
        cq.Workplane("XZ", origin=(BOSS_X, T_WALL, sz * BOSS_Z))
        .circle(BOSS_HOLE_R)
        .extrude(-(BOSS_FACE_Y - T_WALL) - 1)
    )
    csk = cq.Solid.makeCone(
        BOSS_CSK_R + 0.01, 0.0, BOSS_CSK_R + 0.01,
        pnt=cq.Vector(BOSS_X, BOSS_FACE_Y + 0.01, sz * BOSS_Z),
        dir=cq.Vector(0, -1, 0),
    )
    body = body.union(boss).cut(bhole).cut(cq.Workplane("XY").add(csk))

# ---------------- lugs ----------------
ang = math.degrees(math.atan2(LUG_R + LUG_DZ, LUG_CHAMFER_Y))
gr_r = (GR_W ** 2 / 4 + GR_DEPTH ** 2) / (2 * GR_DEPTH)
for sx in (-1, 1):
    for sz in (-1, 1):
        zc = sz * (H / 2 + LUG_DZ)
        z_wall = sz * H / 2
        lug = (
            cq.Workplane("XZ", origin=(sx * LUG_X, 0, zc))
            .circle(LUG_R)
            .extrude(-LUG_L)
        )
        # keep only the part outside the wall
        keep = cq.Workplane("XY").box(40, 40, 20, centered=(True, False, False))
        if sz < 0:
            keep = keep.mirror("XY")
        keep = keep.translate((sx * LUG_X, -5, z_wall - sz * T_WALL * 0.5))
        lug = lug.intersect(keep)
        # inclined front face
        cutter = (
            cq.Workplane("XY")
            .box(30, 30, 30, centered=(True, False, True))
            .translate((0, -30, 0))
        )
        cutter = cutter.rotate((0, 0, 0), (1, 0, 0), -sz * (90 - ang))
        cutter = cutter.translate((sx * LUG_X, 0, z_wall))
        lug = lug.cut(cutter)
        body = body.union(lug)

        # hex pocket in the inclined face, coaxial with the hole
        y_face = LUG_DZ / math.tan(math.radians(ang))
        pocket = (
            cq.Workplane("XZ", origin=(sx * LUG_X, y_face - 3.0, zc))
            .polygon(6, 2 * LUG_POCKET_R)
            .extrude(-(3.0 + LUG_POCKET_D))
        )
        body = body.cut(pocket)

        # groove along the arm, from the lug back face to the rear edge
        groove = (
            cq.Workplane("XZ", origin=(sx * GR_X, LUG_L, sz * (H / 2 + gr_r - GR_DEPTH)))
            .circle(gr_r)
            .extrude(-(D - LUG_L + 1))
        )
        body = body.cut(groove)
        hole = (
            cq.Workplane("XZ", origin=(sx * LUG_X, -1.0, zc))
            .circle(LUG_HOLE_R)
            .extrude(-LUG_L - 2)
        )
        body = body.cut(hole)

# ---------------- edge treatment ----------------
# small round where each lug sits on the wall
for sx in (-1, 1):
    for sz in (-1, 1):
        try:
            body = body.edges(
                box_sel(sx * LUG_X - 6, 0.3, sz * H / 2 - 0.05, sx * LUG_X + 6, LUG_L + 0.05, sz * H / 2 + 0.05)
            ).fillet(LUG_BASE_R)
        except Exception:
            pass
# rounded rear rim of the open back
try:
    body = body.edges(box_sel(-W, D - 0.01, -H, W, D + 0.01, H)).fillet(REAR_R)
except Exception:
    pass

result = body
